import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
T_MAX = 4.1          # thickness at the crown of the top surface
T_SIDE = 2.1         # thickness of the thin outer (-X) shoulder
SLOPE_L = 0.061      # top-surface slope toward the -X side
SLOPE_R = 0.009      # top-surface slope toward the +X side
SLOPE_B = 0.027      # top-surface slope toward the wide rear end
CROWN_X = 6.0        # X of the crown line (at Y_PIVOT)
SLOPE_LY = 0.009     # toward the tip the -X slope face rises (from Y_PIVOT on)
Y_PIVOT = -60.0
REAR_Y0 = 55.0       # where the rear slope starts
RIB_H = 0.9          # rib height above the local top surface
RIB_W = 2.6          # rib width
POCKET_D = 2.0       # depth of the recessed panels
SLOT_L, SLOT_H, SLOT_D = 7.0, 1.4, 5.0   # small side slot near the tip
SLOT_POS = (12.9, -128.0, 2.2)           # slot centre (on the +X side face)
SEAM_Z = 2.0         # the plate is laid up from a base layer and a top layer
RECESS = (5.0, 6.0, 1.2)                 # small recess in the underside near the tip
RECESS_POS = (-3.0, -132.0)

# plan-view outline: right tip corner, up the +X side, round the rear end,
# down the -X side (shoulder) to the left tip corner
OUTLINE = [
    (9.9, -137.2), (12.4, -122.8), (14.6, -111.5), (17.0, -94.5), (21.9, -67.7), (25.2, -47.2),
    (29.1, -33.7), (33.0, -17.2), (36.2, -3.7), (39.3, 10.0), (42.7, 23.6), (45.7, 37.8), (48.3, 53.2),
    (49.6, 69.1), (49.2, 85.0), (47.3, 100.5), (45.1, 110.1), (41.8, 119.5), (37.8, 126.4), (32.6, 133.2),
    (27.8, 138.7), (20.9, 140.0), (12.8, 137.3), (4.5, 131.1), (-3.7, 125.0), (-11.2, 119.3), (-18.9, 113.6),
    (-27.1, 102.6), (-33.9, 91.8), (-40.8, 80.9), (-46.2, 71.3), (-48.7, 63.2), (-48.9, 54.6), (-47.4, 46.3),
    (-42.1, 35.4), (-38.2, 24.6), (-33.0, 13.6), (-29.8, 6.0), (-29.4, 1.5), (-29.8, -11.8), (-29.5, -33.1), (-28.3, -49.6),
    (-26.2, -67.7), (-22.4, -88.1), (-17.7, -108.6), (-12.0, -128.5), (-9.4, -135.6), (-7.3, -138.4),
]
# tip end: straight from the left corner to the notch apex, then a curve to the right corner
TIP_APEX = (0.0, -136.0)
TIP_CURVE = [(2.0, -136.6), (4.3, -137.7), (7.0, -138.2)]

# recessed panels of the narrow front section
POCKET_T = [(-22.0, -0.5), (0.8, 1.0), (2.3, -44.0), (-3.8, -55.0), (-10.5, -54.5)]
POCKET_G2 = [(2.0, -121.0), (-0.4, -62.0), (2.0, -47.0), (15.5, -23.0), (29.5, -7.0),
             (32.0, -9.0), (27.5, -26.0), (21.5, -48.0), (16.5, -72.0), (8.5, -120.0)]
POCKET_G1 = [(-10.8, -57.5), (-3.6, -58.2), (-2.2, -95.0), (-2.8, -121.5), (-7.2, -121.5), (-9.2, -95.0)]
POCKET_FILLET = 1.0  # rounded floor of the recessed panels

# raised ribs of the wide rear section (centre-line polylines)
RIBS = [
    [(-13.0, 1.0), (0.8, 2.0), (10.0, 3.2), (20.0, 4.2), (31.0, 5.0)],                 # cross bar
    [(-11.0, 1.0), (-11.0, 30.0), (-10.8, 54.0)],                                      # long rib
    [(-10.8, 54.0), (-19.5, 65.0)],                                                    # stub
    [(-10.8, 54.0), (0.0, 62.5), (8.2, 67.0)],                                         # branch
    [(15.8, 5.0), (16.0, 30.0), (16.5, 51.7)],                                         # second long rib
    [(24.5, 38.0), (16.5, 51.7), (10.0, 64.2), (8.3, 70.7), (9.9, 75.0), (14.6, 75.7),
     (18.2, 73.8), (22.1, 68.2), (25.5, 60.7), (30.5, 52.0)],                         # arch
    [(9.6, 75.2), (7.0, 83.0)],                                                        # stub
    [(1.0, 2.5), (4.5, 11.0), (10.0, 14.5), (15.8, 8.0)],                              # small arches
    [(15.8, 8.0), (21.5, 14.0), (27.5, 14.5), (31.0, 6.0)],
]
LOOP = ((34.3, 15.5), 3.3, (37.5, 105.0), 6.5)           # tapered ring (c1, r1, c2, r2)


# ---------------------------------------------------------------- helpers
def above(z0, sx=0.0, sy=0.0):
    """Half space Z > z0 + sx*X + sy*Y as a big slab."""
    pl = cq.Plane(origin=(0, 0, z0), xDir=(1, 0, sx), normal=(-sx, -sy, 1.0))
    return cq.Workplane(pl).rect(2000, 2000).extrude(300).val()


def roof_cut(dz=0.0):
    """Everything above the (faceted) top surface raised by dz."""
    top = above(T_MAX + dz)
    right = above(T_MAX + SLOPE_R * CROWN_X + dz, sx=-SLOPE_R)
    rear = above(T_MAX + SLOPE_B * REAR_Y0 + dz, sy=-SLOPE_B)
    left = (above(T_SIDE + dz)
            .intersect(above(T_MAX - SLOPE_L * CROWN_X + dz, sx=SLOPE_L))
            .intersect(above(T_MAX - SLOPE_L * CROWN_X + SLOPE_LY * Y_PIVOT + dz, sx=SLOPE_L, sy=-SLOPE_LY)))
    return top.fuse(right, rear, left).clean()


def outline_wp(h, z0=0.0):
    return (cq.Workplane("XY").workplane(offset=z0).moveTo(*OUTLINE[0])
            .spline(OUTLINE[1:], includeCurrent=True).lineTo(*TIP_APEX)
            .spline(TIP_CURVE + [OUTLINE[0]], includeCurrent=True).close().extrude(h))


def z_roof(x, y):
    """Height of the faceted top surface at (x, y)."""
    return min(T_MAX,
               T_MAX - SLOPE_R * (x - CROWN_X),
               T_MAX - SLOPE_B * (y - REAR_Y0),
               max(T_SIDE, T_MAX + SLOPE_L * (x - CROWN_X),
                   T_MAX + SLOPE_L * (x - CROWN_X) - SLOPE_LY * (y - Y_PIVOT)))


def rib_path(pts, w, h, z0=0.0):
    """Union of round-ended slots along a centre-line polyline, extruded h from z0."""
    body = None
    for (xa, ya), (xb, yb) in zip(pts[:-1], pts[1:]):
        L = math.hypot(xb - xa, yb - ya)
        ang = math.degrees(math.atan2(yb - ya, xb - xa))
        seg = (cq.Workplane("XY").workplane(offset=z0).center((xa + xb) / 2, (ya + yb) / 2)
               .slot2D(L + w, w, ang).extrude(h))
        body = seg if body is None else body.union(seg)
    return body


def loop_path(c1, r1, c2, r2, n_arc=5):
    """Closed centre-line polyline of a tapered ring (rib centred inside the outer boundary)."""
    (x1, y1), (x2, y2) = c1, c2
    r1, r2 = r1 - RIB_W / 2.0, r2 - RIB_W / 2.0
    d = math.hypot(x2 - x1, y2 - y1)
    base = math.atan2(y2 - y1, x2 - x1)
    phi = math.acos((r1 - r2) / d)
    pts = []
    for i in range(n_arc + 1):          # around the far end
        a = base + phi - 2 * phi * i / n_arc
        pts.append((x2 + r2 * math.cos(a), y2 + r2 * math.sin(a)))
    for i in range(n_arc + 1):          # around the near end
        a = base - phi - 2 * (math.pi - phi) * i / n_arc
        pts.append((x1 + r1 * math.cos(a), y1 + r1 * math.sin(a)))
    pts.append(pts[0])
    return pts


def rounded_poly(pts, r, h, z0=0.0):
    w = cq.Workplane("XY").workplane(offset=z0).polyline(pts).close()
    return w.offset2D(-r).offset2D(r).extrude(h)


def floor_edges(solid):
    """Edges where a (near) vertical wall meets a floor face, below the top surface."""
    faces = solid.Faces()
    out = []
    for e in solid.Edges():
        adj = [f for f in faces if any(e.isSame(fe) for fe in f.Edges())]
        kinds = [abs(f.normalAt().z) < 0.2 for f in adj]
        if len(kinds) == 2 and kinds[0] != kinds[1] and e.Center().z < T_MAX:
            out.append(e)
    return out


def fillet_floor(wp, r):
    res = []
    for so in wp.val().Solids():
        for rr in (r, 0.6 * r):
            try:
                so = so.fillet(rr, floor_edges(so))
                break
            except Exception:
                pass
        res.append(so)
    return cq.Compound.makeCompound(res)


# ---------------------------------------------------------------- plate
H_BIG = 12.0
base = outline_wp(SEAM_Z)
upper = outline_wp(H_BIG - SEAM_Z, SEAM_Z).cut(roof_cut(0.0))
plate = base.union(upper, clean=False)

# recessed panels (floor follows the top surface)
pock = (rounded_poly(POCKET_T, 2.0, 20, -2)
        .union(rounded_poly(POCKET_G2, 2.0, 20, -2))
        .union(rounded_poly(POCKET_G1, 2.0, 20, -2)))
pock = pock.intersect(cq.Workplane().add(roof_cut(-POCKET_D)))
pock = cq.Workplane().add(fillet_floor(pock, POCKET_FILLET))
plate = plate.cut(pock, clean=False)

# raised ribs (flat crest following the top surface, RIB_H above it)
ribs = None
for path in RIBS + [loop_path(*LOOP)]:
    r = rib_path(path, RIB_W, H_BIG, 0.5)
    ribs = r if ribs is None else ribs.union(r)
ribs = ribs.cut(cq.Workplane().add(roof_cut(RIB_H))).intersect(outline_wp(H_BIG))
plate = plate.union(ribs, clean=False)


# small slot in the +X side face near the tip
slot = cq.Workplane("XY").box(SLOT_D * 2, SLOT_L, SLOT_H).translate(SLOT_POS)
plate = plate.cut(slot, clean=False)

# small recess in the underside near the tip
recess = cq.Workplane("XY").box(*RECESS).translate((RECESS_POS[0], RECESS_POS[1], RECESS[2] / 2 - 0.01))
plate = plate.cut(recess, clean=False)

result = plate
VIEW = {"azimuth": 45, "elevation": 26}
